import cadquery as cq
import math

# Tilted cradle / angled mount: a lofted body on a turned square base whose top is a plane
# tilted ~26 deg, carrying an open-ended pocket with rims, stop bars and three through holes
# (counterbored from the base).

# ======================= parameters (mm) =======================

# tilted top planes  h(x,y) = C + G * (x*UX + y*UY)
PSI = -30.0                    # plan direction in which the top rises
G = 0.48                       # slope of the top planes
C_TOP = 46.0                   # construction plane for the loft (above all)
C_RIM = 41.9                   # NE rim top (its plane is a little steeper)
G_RIM = 0.50
C_FLOOR = 30.5                 # pocket floor
C_PAD = 32.1                   # ledge at the E corner and along the SE edge
C_SW = 35.8                    # low SW rim
C_SBAR = 40.7                  # south stop bar
C_WBAR = 42.5                  # west stop bar
H_CAP = 43.4                   # horizontal flat along the SE edge

NE_CHAMFER = 3.0               # chamfer on the outer top edge of the NE rim
SB_CHAMFER = 3.0               # chamfer on the outer top edge of the S bar

# holes: (floor point, bottom point) in plan - an equilateral pattern of ~38 mm
HOLES = [((5.0, 11.9), (16.0, 5.6)), ((-29.3, -2.5), (-22.5, -6.7)), ((-5.1, -23.6), (7.7, -31.2))]
HOLE_D = 2.2                   # through hole
CBORE_D = 5.4                  # counterbore from the bottom
CBORE_DEPTH_BELOW_FLOOR = 6.0  # material left under the floor

UX, UY = math.cos(math.radians(PSI)), math.sin(math.radians(PSI))
COSA = 1.0 / math.sqrt(1.0 + G * G)
A2 = (math.cos(math.radians(PSI + 90)), math.sin(math.radians(PSI + 90)))   # horizontal in-plane dir
N_UP = cq.Vector(-G * UX, -G * UY, 1.0).normalized()


def pu(x, y):
    return x * UX + y * UY


def hpl(c, x, y, g=G):
    return c + g * pu(x, y)


# ======================= base + loft body =======================
# bottom outline (hexagon: a square of ~68 mm turned 30 deg with the N and W corners pulled in)
S_b = (14.8, -43.5)
E_b = (50.1, 15.1)
K_N = (1.7, 42.3)
N_b = (-16.5, 48.3)
W_b = (-47.4, -4.1)
K_W = (-32.6, -17.5)


def lerp(p, q, t):
    return (p[0] + (q[0] - p[0]) * t, p[1] + (q[1] - p[1]) * t)


# side edges: (bottom point, observed point (x, y, z), k)
# the edges are curves leaving the base with slope k*(mean slope) and bending over (k=1: straight)
rulings = [
    (E_b, (39.6, 13.5, 43.4), 0.35),
    (K_N, (-2.6, 44.1, 28.2), 0.5),
    (N_b, (-19.2, 50.0, 19.5), 0.5),
    (W_b, (-50.1, -2.3, 19.6), 0.8),
    (K_W, (-40.3, -18.0, 28.0), 0.6),
    (S_b, (-9.6, -49.2, 46.2), 0.5),
    (lerp(S_b, E_b, 0.205), (23.3, -31.6, 43.4), 0.5),
    (lerp(S_b, E_b, 0.22), (17.4, -24.7, 43.4), 0.35),
]
C_MID, G_MID = C_TOP * 0.45, G * 0.45     # intermediate loft section plane


def edge_point(b, o, k, c, g):
    """point of the side edge curve (b -> o) where it meets the plane h = c + g*(p.u)"""
    bx, by = b
    ox, oy, oz = o
    dx, dy = ox - bx, oy - by

    def at(z):
        t = z / oz
        f = k * t + (1.0 - k) * t * t
        return bx + f * dx, by + f * dy

    z = c
    for _ in range(60):
        x, y = at(z)
        z = c + g * pu(x, y)
    x, y = at(z)
    return cq.Vector(x, y, z)


bot_w = cq.Wire.makePolygon([cq.Vector(b[0], b[1], 0) for b, o, k in rulings], close=True)
mid_w = cq.Wire.makePolygon([edge_point(b, o, k, C_MID, G_MID) for b, o, k in rulings], close=True)
top_w = cq.Wire.makePolygon([edge_point(b, o, k, C_TOP, G) for b, o, k in rulings], close=True)
loft = cq.Workplane("XY").add(cq.Solid.makeLoft([bot_w, mid_w, top_w], False))


# ======================= helpers for the tilted frame =======================
def floor_plane(c=C_FLOOR):
    return cq.Plane(origin=cq.Vector(0, 0, c), xDir=cq.Vector(A2[0], A2[1], 0), normal=N_UP)


def to_local(p):
    """plan point -> local coords on the tilted planes (vertical projection)"""
    return (p[0] * A2[0] + p[1] * A2[1], -pu(p[0], p[1]) / COSA)


def below(c, g=G):
    n = cq.Vector(-g * UX, -g * UY, 1.0).normalized()
    pl = cq.Plane(origin=cq.Vector(0, 0, c), xDir=cq.Vector(A2[0], A2[1], 0), normal=n)
    return cq.Workplane(pl).rect(500, 500).extrude(-200)


def nprism(pts, c, lo=-80.0, hi=60.0):
    """prism normal to the tilted planes; the plan polygon is exact on the plane with offset c"""
    loc = [to_local(p) for p in pts]
    return cq.Workplane(floor_plane(c)).workplane(offset=lo).polyline(loc).close().extrude(hi - lo)


def vprism(pts):
    return cq.Workplane("XY").workplane(offset=-5).polyline(pts).close().extrude(100)


# ======================= plan regions (measured from the top view) =======================
R_NE = [(-33.3, 51.6), (-20.3, 44.1), (-14.6, 41.6), (-4.7, 38.4), (-2.6, 34.3), (7.3, 28.1),
        (8.3, 25.4), (18.7, 19.7), (21.6, 24.9), (34.3, 41.0), (0.0, 70.0), (-45.0, 62.0)]
R_SW = [(-36.7, -12.0), (-35.1, -13.5), (-15.2, -30.2), (-12.5, -30.5), (-9.0, -41.0),
        (-14.7, -45.0), (-24.0, -60.0), (-62.0, -22.0), (-40.6, -15.9)]
R_SB = [(-14.7, -43.3), (6.5, -30.2), (10.0, -36.8), (14.0, -44.0), (-9.6, -60.0), (-20.0, -60.0)]
R_WT = [(-45.4, 5.2), (-37.9, 0.4), (-38.1, -3.0), (-49.8, -2.0), (-58.0, -2.7), (-58.0, 12.0)]
R_WB = [(-38.1, -3.0), (-36.7, -12.0), (-40.6, -15.9), (-44.9, -13.0), (-45.5, -5.5)]
R_WC = [(-49.8, -2.0), (-45.5, -5.5), (-44.9, -13.0), (-50.0, -24.0), (-58.0, -11.0), (-58.0, -2.7)]
# W tab: ridge line and the low W corner point of its sloped outer facet (x, y, z)
W_RIDGE = ((-46.9, -0.3), (-38.1, -3.0))
W_CORNER = (-49.8, -2.0, 19.2)
R_PAD = [(18.7, 19.7), (21.1, 16.2), (33.0, 9.0), (9.6, -29.0), (8.0, -30.6), (6.5, -30.2), (10.0, -36.8),
         (14.0, -44.0), (40.0, -30.0), (70.0, 20.0), (40.0, 35.0), (21.6, 24.9)]
R_CAP = [  # horizontal flat along the SE edge
        (33.1, 8.8), (9.6, -29.0), (8.0, -30.6), (6.5, -30.2), (10.0, -36.8), (14.0, -44.0),
         (40.0, -30.0), (70.0, 20.0), (40.0, 30.0)]

def plane_slab(p1, p2, p3, keep):
    """big solid on the far side (away from point `keep`) of the plane through p1, p2, p3"""
    a, b, c = cq.Vector(*p1), cq.Vector(*p2), cq.Vector(*p3)
    n = (b - a).cross(c - a).normalized()
    if n.dot(cq.Vector(*keep) - a) > 0:
        n = -n
    pl = cq.Plane(origin=a, xDir=(b - a).normalized(), normal=n)
    return cq.Workplane(pl).rect(400, 400).extrude(80)


def chamfer_slab(pa, pb, outward, c_top, size, g=G):
    """solid to cut a 45 deg chamfer of the given size along an outer top edge (plan line pa-pb)
    of a feature whose top lies on the tilted plane with offset c_top"""
    dx, dy = pb[0] - pa[0], pb[1] - pa[1]
    ln = math.hypot(dx, dy)
    dx, dy = dx / ln, dy / ln
    d3 = cq.Vector(dx, dy, g * pu(dx, dy)).normalized()
    n_up = cq.Vector(-g * UX, -g * UY, 1.0).normalized()
    o3 = n_up.cross(d3)
    if o3.x * outward[0] + o3.y * outward[1] < 0:
        o3 = -o3
    o3 = o3.normalized()
    # line L: the outer edge moved inwards by `size` (measured along the top plane)
    hl = math.hypot(o3.x, o3.y)
    p0 = (pa[0] - size * o3.x / (hl * hl), pa[1] - size * o3.y / (hl * hl))
    origin = cq.Vector(p0[0], p0[1], hpl(c_top, p0[0], p0[1], g))
    v = (o3 - n_up).normalized()
    n = d3.cross(v)
    if n.dot(o3 + n_up) < 0:
        n = -n
    pl = cq.Plane(origin=origin, xDir=d3, normal=n)
    return cq.Workplane(pl).rect(400, 400).extrude(80)


core = loft.intersect(below(C_FLOOR))
ne = loft.intersect(nprism(R_NE, C_RIM - 0.7)).intersect(below(C_RIM, G_RIM))
ne = ne.cut(chamfer_slab((-2.6, 44.1), (21.8, 24.4), (0.628, 0.778), C_RIM, NE_CHAMFER, G_RIM))
ne = ne.cut(chamfer_slab((-19.2, 50.0), (-2.6, 44.1), (0.335, 0.943), C_RIM, NE_CHAMFER, G_RIM))
sw = loft.intersect(nprism(R_SW, C_SW)).intersect(below(C_SW))
sb = loft.intersect(nprism(R_SB, C_SBAR)).intersect(below(C_SBAR))
sb = sb.cut(chamfer_slab((-9.6, -49.2), (12.5, -37.3), (0.47, -0.883), C_SBAR, SB_CHAMFER))
pad = loft.intersect(nprism(R_PAD, C_PAD)).intersect(below(C_PAD))
wt = loft.intersect(nprism(R_WT, C_WBAR)).intersect(below(C_WBAR))
wt = wt.cut(plane_slab(W_RIDGE[0] + (hpl(C_WBAR, *W_RIDGE[0]),), W_RIDGE[1] + (hpl(C_WBAR, *W_RIDGE[1]),),
                       W_CORNER, (-45.0, 3.0, 10.0)))
wb = loft.intersect(nprism(R_WB, C_WBAR)).intersect(below(C_WBAR))
wc = loft.intersect(nprism(R_WC, C_RIM)).intersect(below(C_RIM, G_RIM))

body = core.union(ne).union(pad).union(sw).union(wt).union(wb).union(wc)
cap = vprism(R_CAP).intersect(
    cq.Workplane("XY").box(300, 300, 100, centered=(True, True, False)).translate((0, 0, H_CAP)))
body = body.cut(cap).union(sb)

# ======================= holes =======================
# each hole: floor point (plan) and bottom point (plan); through hole + counterbore from below
for (fx, fy), (bx, by) in HOLES:
    top = cq.Vector(fx, fy, hpl(C_FLOOR, fx, fy))
    bot = cq.Vector(bx, by, 0.0)
    axis = (top - bot).normalized()
    length = (top - bot).Length
    start = bot - axis * 5.0
    pl = cq.Plane(origin=start, xDir=axis.cross(cq.Vector(0, 0, 1)).normalized(), normal=axis)
    thru = cq.Workplane(pl).circle(HOLE_D / 2).extrude(length + 15.0)
    cb = cq.Workplane(pl).circle(CBORE_D / 2).extrude(5.0 + length - CBORE_DEPTH_BELOW_FLOOR)
    body = body.cut(thru).cut(cb)

result = body
